import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire

# ============ driving dimensions (mm) ============
PLATE_W = 130.0          # flange length (X)
PLATE_D = 99.5           # flange depth (Y)
PLATE_T = 2.0            # flange thickness
PLATE_R = 8.0            # flange corner radius
WALL = 1.7               # hopper wall thickness
CORNER_R_IN = 1.0        # inside radius of the hopper corner
CORNER_R_OUT = CORNER_R_IN + WALL   # outside radius (concentric)

# hopper opening = ellipse + sharp corner joined by two tangent lines
ELL_C = (-0.3, 0.09)     # ellipse centre
ELL_A = 54.1             # semi major axis
ELL_B = 33.7             # semi minor axis
ELL_ROT = 5.8            # deg
CORNER = (-60.4, 44.9)   # sharp corner of the opening (inside of wall)

FLOOR_Z = -63.8          # flat floor level (outside)
TIP_Z = -135.0           # bottom of the spout

# spout / funnel: (z, p, q) = height, reach along the back wall, reach along
# the left wall, both measured from the outside corner (outside surface)
FUNNEL = [
    (-135.0, 13.0, 4.0),
    (-115.0, 15.8, 5.7),
    (-95.0, 21.8, 8.9),
    (-80.0, 30.6, 14.8),
    (-70.0, 39.3, 24.2),
    (-62.5, 54.0, 43.0),
]

# raised ramp of the floor on the far side (away from the spout): cylindrical
# surface rising along direction RAMP_ANG, starting at RAMP_W0 from the origin
RAMP_ANG = -31.0         # deg
RAMP_W0 = 1.6
RAMP_R = 125.0
RAMP_DIR = (math.cos(math.radians(RAMP_ANG)), math.sin(math.radians(RAMP_ANG)))

# floor slot
SLOT_C = (41.15, -0.6)
SLOT_L = 25.0
SLOT_W = 2.0
SLOT_ANG = -3.9          # deg, rotation of the slot from the Y axis

# flange features
RECT_C = (-47.3, -31.4)
RECT_L = 30.0
RECT_W = 10.0
RECT_ANG = -45.0
HOLES = [(45.8, -35.6), (54.0, -35.6)]
HOLE_D = 5.0

BIG = 95.0


# ============ geometry helpers ============
def ell_tangent_points(c, a, b):
    """Tangent points on the (rotated) opening ellipse seen from point c."""
    ang = math.radians(ELL_ROT)
    ca, sa = math.cos(ang), math.sin(ang)
    dx, dy = c[0] - ELL_C[0], c[1] - ELL_C[1]
    lx, ly = ca * dx + sa * dy, -sa * dx + ca * dy
    px, py = lx / a, ly / b
    r = math.hypot(px, py)
    phi = math.atan2(py, px)
    al = math.acos(1.0 / r)
    pts = []
    for th in (phi + al, phi - al):
        ex, ey = a * math.cos(th), b * math.sin(th)
        pts.append((ELL_C[0] + ca * ex - sa * ey, ELL_C[1] + sa * ex + ca * ey))
    return pts


def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


# wall directions from the corner (inside profile)
_T_LEFT, _T_TOP = ell_tangent_points(CORNER, ELL_A, ELL_B)
U_TOP = unit((_T_TOP[0] - CORNER[0], _T_TOP[1] - CORNER[1]))
U_LEFT = unit((_T_LEFT[0] - CORNER[0], _T_LEFT[1] - CORNER[1]))


def offset_corner(d):
    """Corner of the profile grown outward by d."""
    n_top = (-U_TOP[1], U_TOP[0])           # outward normal of back wall
    n_left = (U_LEFT[1], -U_LEFT[0])        # outward normal of left wall
    p = (CORNER[0] + d * n_top[0], CORNER[1] + d * n_top[1])
    q = (CORNER[0] + d * n_left[0], CORNER[1] + d * n_left[1])
    det = U_TOP[0] * (-U_LEFT[1]) - U_TOP[1] * (-U_LEFT[0])
    rx, ry = q[0] - p[0], q[1] - p[1]
    s = (rx * (-U_LEFT[1]) - ry * (-U_LEFT[0])) / det
    return (p[0] + s * U_TOP[0], p[1] + s * U_TOP[1])


C_OUT = offset_corner(WALL)


def teardrop_prism(d, z_top, z_bot, fillet=0.0):
    """Prism of the opening profile grown by d between z_bot and z_top:
    elliptic belly + the triangle spanned by the corner and the two tangent
    points (straight left and back walls)."""
    a, b = ELL_A + d, ELL_B + d
    c = offset_corner(d)
    t_left, t_top = ell_tangent_points(c, a, b)
    h = z_top - z_bot
    ell = (cq.Workplane("XY").workplane(offset=z_bot)
           .center(*ELL_C).ellipse(a, b, rotation_angle=ELL_ROT).extrude(h))
    tri = (cq.Workplane("XY").workplane(offset=z_bot)
           .polyline([c, t_top, ELL_C, t_left]).close().extrude(h))
    s = ell.union(tri).clean()
    if fillet > 0:
        s = s.edges("|Z").edges(
            cq.selectors.NearestToPointSelector((c[0], c[1], (z_top + z_bot) / 2))
        ).fillet(fillet)
    return s


def skew_ellipse_wire(z, p, q, t0=225.0):
    """Exact ellipse through C_OUT + p*U_TOP and C_OUT + q*U_LEFT: the affine
    image of a rational quadratic NURBS circle, so every section of the loft
    shares the same parametrisation (seam placed outside the hopper)."""
    poles = TColgp_Array1OfPnt(1, 9)
    wts = TColStd_Array1OfReal(1, 9)
    for k in range(9):
        a = math.radians(t0 + 45.0 * k)
        r = 1.0 if k % 2 == 0 else math.sqrt(2.0)
        cx, cy = r * math.cos(a), r * math.sin(a)
        x = C_OUT[0] + p * cx * U_TOP[0] + q * cy * U_LEFT[0]
        y = C_OUT[1] + p * cx * U_TOP[1] + q * cy * U_LEFT[1]
        poles.SetValue(k + 1, gp_Pnt(x, y, z))
        wts.SetValue(k + 1, 1.0 if k % 2 == 0 else math.sqrt(0.5))
    knots = TColStd_Array1OfReal(1, 5)
    mults = TColStd_Array1OfInteger(1, 5)
    for i, (kv, m) in enumerate([(0.0, 3), (1.0, 2), (2.0, 2), (3.0, 2), (4.0, 3)]):
        knots.SetValue(i + 1, kv)
        mults.SetValue(i + 1, m)
    crv = Geom_BSplineCurve(poles, wts, knots, mults, 2)
    edge = BRepBuilderAPI_MakeEdge(crv).Edge()
    return cq.Wire(BRepBuilderAPI_MakeWire(edge).Wire())


def funnel_solid(inset, z_shift, z_low_extra):
    """Lofted horn of the spout, shrunk by 'inset' (approximate normal offset)."""
    wires = []
    for i, (z, p, q) in enumerate(FUNNEL):
        zz = z + z_shift
        if i == 0:
            zz -= z_low_extra
        wires.append(skew_ellipse_wire(zz, max(p - inset, 0.6), max(q - inset, 0.6)))
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, ruled=False))


def ramp_cut(d):
    """Material below the ramp surface (offset upward by d for the cavity)."""
    ux, uy = RAMP_DIR
    pl = cq.Plane(origin=(0, 0, 0), xDir=(ux, uy, 0), normal=(uy, -ux, 0))
    r = RAMP_R - d
    zc = FLOOR_Z - 0.5 + RAMP_R
    a = math.radians(45)
    u_end = RAMP_W0 + r * math.sin(a)
    z_end = zc - r * math.cos(a)
    wp = (cq.Workplane(pl).moveTo(RAMP_W0, zc - r)
          .threePointArc((RAMP_W0 + r * math.sin(a / 2), zc - r * math.cos(a / 2)),
                         (u_end, z_end))
          .lineTo(u_end + 60, z_end).lineTo(u_end + 60, -150)
          .lineTo(RAMP_W0, -150).close())
    return wp.extrude(BIG, both=True)


def hopper(d_prism, inset, z_top, floor_z, z_shift, z_low_extra, fillet):
    prism = teardrop_prism(d_prism, z_top, TIP_Z - 20.0, fillet)
    above = (cq.Workplane("XY").workplane(offset=floor_z)
             .rect(2 * BIG, 2 * BIG).extrude(z_top + 5 - floor_z))
    keep = above.union(funnel_solid(inset, z_shift, z_low_extra))
    s = prism.intersect(keep)
    s = s.cut(ramp_cut(inset))
    return s


# ============ flange plate (opening is cut together with the cavity) ============
plate = (cq.Workplane("XY").workplane(offset=-PLATE_T)
         .rect(PLATE_W, PLATE_D).extrude(PLATE_T)
         .edges("|Z").fillet(PLATE_R))
rect_cut = (cq.Workplane("XY").workplane(offset=-PLATE_T - 1.0)
            .center(*RECT_C).rect(RECT_L, RECT_W).extrude(PLATE_T + 2.0)
            .rotate((RECT_C[0], RECT_C[1], 0), (RECT_C[0], RECT_C[1], 1), RECT_ANG))
plate = plate.cut(rect_cut)
plate = plate.cut(cq.Workplane("XY").workplane(offset=-PLATE_T - 1.0)
                  .pushPoints(HOLES).circle(HOLE_D / 2).extrude(PLATE_T + 2.0))

# ============ hopper body ============
# outside of the hopper (top sunk into the plate to avoid coplanar faces)
outer = hopper(WALL, 0.0, -PLATE_T / 2, FLOOR_Z, 0.0, 0.0, CORNER_R_OUT)
# cavity: inside of the walls / floor / funnel, open at the top and the tip
inner = hopper(0.0, WALL, 1.0, FLOOR_Z + WALL, WALL * 0.5, 8.0, CORNER_R_IN)

part = plate.union(outer).cut(inner)

# slot through the raised part of the floor, cut square to the ramp surface
_ux, _uy = RAMP_DIR
_u = _ux * SLOT_C[0] + _uy * SLOT_C[1] - RAMP_W0
_slope = _u / math.sqrt(RAMP_R ** 2 - _u ** 2)
_zs = FLOOR_Z - 0.5 + RAMP_R - math.sqrt(RAMP_R ** 2 - _u ** 2)
slot = (cq.Workplane("XY").box(SLOT_W, SLOT_L, 20.0)
        .rotate((0, 0, 0), (0, 0, 1), SLOT_ANG)
        .rotate((0, 0, 0), (-_uy, _ux, 0), -math.degrees(math.atan(_slope)))
        .translate((SLOT_C[0], SLOT_C[1], _zs)))
part = part.cut(slot)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
